import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 150.0            # body height (bottom face z=0 to top face z=H)
R_BOT = 24.5         # outer radius at the bottom
R_TOP = 21.45        # outer radius at the (flared) top edge
SLOPE = 0.0324       # radial taper of the cone (mm radius per mm height)
Z_FLARE = 129.0      # height where the concave top flare starts
WALL = 3.1           # wall thickness

# top collar (C-shaped lip standing above the top face)
COL_RO = 18.4          # flush with the bore edge
COL_RI = 16.4
COL_H = 3.2            # height above the top face
COL_CH = 0.75          # chamfer on the outer top edge
COL_IN_H = 2.1         # height of the vertical inner face of the lip
COL_UNDER = 1.4        # slope (dz/dr) of the conical overhang under the lip
GAP_HALF = 55.0        # half angle of the collar gap, centred on -Y (deg)

# internal strip holder behind the front wall (-Y side): a plate spanning the
# bore whose back face follows the outer wall profile (extruded along X) and a
# planar slot floor; the strip slot between plate and wall is open top and bottom
SLOT_Y_TOP = -12.9     # slot floor (plate front face) y at the holder top
SLOT_TILT = 0.0186     # outward lean of the slot floor per mm of depth
D_BACK = 9.95          # plate back face offset from outer wall profile
PLATE_RECESS = 2.0     # top of the holder sits this far below the top face
SLOT_HALF_W = 10.7     # half width of the strip slot (x)
PLATE_Z0 = 3.0         # holder stops this far above the bottom face
BLOCK_HALF_W = 12.2    # half width of the holder block at its back face
BLOCK_SIDE_Y = -10.4   # y where the block's slanted side faces start
BLOCK_SIDE_K = 0.325   # side face flare (dx per dy) towards the front wall

# column of holes on the front (-Y) face
HOLE_D = 4.2
HOLE_TOP_Z = H - 5.6
HOLE2_Z = H - 15.6
HOLE_LAST_Z = 6.0
N_HOLES = 13

# very shallow flats on the front face around the hole column
FLAT_DEPTH = 0.115
FLATS = [(52.8, 128.0), (-1.0, 41.0)]   # (z_low, z_high)


def outer_r(z):
    """outer radius of the body at height z (cone + tangent concave flare)"""
    r = R_BOT - SLOPE * z
    if z > Z_FLARE:
        a = (R_TOP - (R_BOT - SLOPE * H)) / (H - Z_FLARE) ** 2
        r += a * (z - Z_FLARE) ** 2
    return r


def profile_pts(offset, z0, z1, n_lo=4, n_hi=7):
    """sample points (r - offset, z) along the wall profile"""
    zs = []
    for i in range(n_lo):
        zs.append(z0 + (min(Z_FLARE, z1) - z0) * i / n_lo)
    if z1 > Z_FLARE:
        for i in range(n_hi + 1):
            zs.append(Z_FLARE + (z1 - Z_FLARE) * i / n_hi)
    else:
        zs.append(z1)
    return [(outer_r(z) - offset, z) for z in zs]


def slope_at(z):
    h = 1e-4
    return (outer_r(z + h) - outer_r(z - h)) / (2 * h)


def revolve_profile(offset, z0, z1, top_ext=0.0):
    pts = profile_pts(offset, z0, z1)
    t0 = (slope_at(z0), 1.0)
    t1 = (slope_at(z1), 1.0)
    wp = cq.Workplane("XZ").moveTo(0, z0).lineTo(pts[0][0], z0)
    wp = wp.spline(pts[1:], tangents=[t0, t1], includeCurrent=True)
    if top_ext > 0:
        wp = wp.lineTo(pts[-1][0], z1 + top_ext)
        wp = wp.lineTo(0, z1 + top_ext)
    else:
        wp = wp.lineTo(0, z1)
    solid = wp.close().revolve(360, (0, 0, 0), (0, 1, 0))
    # put the revolve seam on the front (-Y) side, along the hole column
    return solid.rotate((0, 0, 0), (0, 0, 1), -90)


def front_prism(offset, x_half, z0, z1):
    """prism on the -Y side bounded by the surface y = -(outer_r(z) - offset)"""
    pts = [(-(r), z) for (r, z) in profile_pts(offset, z0, z1)]
    far = -60.0
    t0 = (-slope_at(z0), 1.0)
    t1 = (-slope_at(z1), 1.0)
    wp = (
        cq.Workplane("YZ", origin=(-x_half, 0, 0))
        .moveTo(far, z0)
        .lineTo(pts[0][0], z0)
        .spline(pts[1:], tangents=[t0, t1], includeCurrent=True)
        .lineTo(far, z1)
        .close()
    )
    return wp.extrude(2 * x_half)


# ---------------- outer body and cavity ----------------
outer = revolve_profile(0.0, 0.0, H)
ext = 2.0
cavity = revolve_profile(WALL, -ext, H, top_ext=ext)

# strip holder: block filling the front of the bore minus the strip slot
block = front_prism(D_BACK, 2 * R_BOT, PLATE_Z0, H - PLATE_RECESS)
y_far = -2 * R_BOT
x_far = BLOCK_HALF_W + BLOCK_SIDE_K * (BLOCK_SIDE_Y - y_far)
side_limit = (
    cq.Workplane("XY", origin=(0, 0, -5))
    .polyline([
        (BLOCK_HALF_W, 0), (BLOCK_HALF_W, BLOCK_SIDE_Y), (x_far, y_far),
        (-x_far, y_far), (-BLOCK_HALF_W, BLOCK_SIDE_Y), (-BLOCK_HALF_W, 0),
    ])
    .close()
    .extrude(H + 15)
)
block = block.intersect(side_limit)
z_pt = H - PLATE_RECESS


def slot_y(z):
    return SLOT_Y_TOP - SLOT_TILT * (z_pt - z)


z_lo, z_hi = -ext - 1.0, H + ext + 1.0
slot = (
    cq.Workplane("YZ", origin=(-SLOT_HALF_W, 0, 0))
    .polyline([(slot_y(z_lo), z_lo), (slot_y(z_hi), z_hi), (-60, z_hi), (-60, z_lo)])
    .close()
    .extrude(2 * SLOT_HALF_W)
)
cavity = cavity.cut(block.cut(slot))

body = outer.cut(cavity)

# ---------------- C-shaped collar ----------------
z_a = H + COL_H - COL_IN_H
r_anchor = COL_RO + 0.6          # buried part that fuses the lip into the wall
z_g = z_a - (r_anchor - COL_RI) * COL_UNDER
lip_prof = (
    cq.Workplane("XZ")
    .polyline([
        (COL_RI, z_a),
        (COL_RI, H + COL_H),
        (COL_RO - COL_CH, H + COL_H),
        (COL_RO, H + COL_H - COL_CH),
        (COL_RO, H - 0.5),
        (r_anchor, H - 0.5),
        (r_anchor, z_g),
    ])
    .close()
)
lip = lip_prof.revolve(360.0 - 2 * GAP_HALF, (0, 0, 0), (0, 1, 0))
lip = lip.rotate((0, 0, 0), (0, 0, 1), -90.0 + GAP_HALF)
body = body.union(lip)

# ---------------- shallow flats around the hole column ----------------
for (zl, zh) in FLATS:
    r_l, r_h = R_BOT - SLOPE * zl - FLAT_DEPTH, R_BOT - SLOPE * zh - FLAT_DEPTH
    flat = (
        cq.Workplane("YZ", origin=(-6, 0, 0))
        .polyline([(-r_l, zl), (-r_h, zh), (-40, zh), (-40, zl)])
        .close()
        .extrude(12)
    )
    body = body.cut(flat)

# ---------------- hole column on the front face ----------------
zs = [HOLE_TOP_Z] + [
    HOLE2_Z - i * (HOLE2_Z - HOLE_LAST_Z) / (N_HOLES - 2) for i in range(N_HOLES - 1)
]
for z in zs:
    r_in = outer_r(z) - WALL
    y0 = -(r_in - 0.8)
    depth = outer_r(z) + 3.0 + y0
    h = (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .center(0, z)
        .circle(HOLE_D / 2.0)
        .extrude(depth)
    )
    body = body.cut(h)

result = body
